import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 78.0            # axial length of the cone (small end at y=0, large end at y=L)
R_SMALL = 18.65     # outer radius at the small (threaded) end
R_LARGE = 60.0      # outer radius at the large open end
T_WALL_RIM = 2.0    # wall thickness (normal to surface) at the large open rim
T_WALL_HUB = 2.7    # wall thickness (normal to surface) where the cone leaves the hub
RIM_EDGE_R = 0.5    # round-over on the large rim edges

THREAD_MINOR = 15.35  # internal thread minor radius
THREAD_MAJOR = 16.7   # internal thread major radius
THREAD_PITCH = 3.0
THREAD_TURNS = 2.5    # turns of the helical thread groove
THREAD_START = 0.4    # axial start of the thread helix
THREAD_GROOVE_W = 2.6 # groove width at the bore (crest gap)
THREAD_ROOT_W = 1.0   # groove width at the root (major radius)
HUB_LEN = 10.0        # axial position where the hub shoulder meets the cone wall
ENTRY_CHAMFER = 0.3   # chamfer at the thread entry

N_SLOTS = 8
SLOT_YC = 18.0        # axial position of slot centre (from small end)
SLOT_SPAN = 22.2      # distance between slot end-centres (in sketch plane)
SLOT_W = 4.1          # slot width
SLOT_ANGLE = 24.7     # slot inclination from circumferential direction (deg)
SLOT_EDGE_R = 0.4     # round-over on the slot edges (outside and inside)

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
tan_a = (R_LARGE - R_SMALL) / L
alpha = math.atan(tan_a)
ca = math.cos(alpha)


def r_out(y):
    return R_SMALL + tan_a * y


def r_in(y):
    # inner cone: wall tapers linearly from the hub to the rim
    f = (y - HUB_LEN) / (L - HUB_LEN)
    t = T_WALL_HUB + (T_WALL_RIM - T_WALL_HUB) * f
    return r_out(y) - t / ca


# ---------------- revolved body ----------------
# half-section in (r, y): r along X, rotation axis along Y
pts = [
    (R_SMALL, 0.0),
    (R_LARGE, L),
    (r_in(L), L),
    (r_in(HUB_LEN), HUB_LEN),
    (THREAD_MINOR, HUB_LEN),              # hub shoulder down to the threaded bore
    (THREAD_MINOR, ENTRY_CHAMFER),
    (THREAD_MINOR + ENTRY_CHAMFER, 0.0),  # small chamfer at the thread entry
]
body = (
    cq.Workplane("XY")
    .polyline(pts)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), 180.0)   # park the revolve seam on the far (-X) side
)
# small round-over on both edges of the large open rim
rim_edges = [
    e for e in body.val().Edges()
    if e.geomType() == "CIRCLE" and abs(e.Center().y - L) < 1e-3
]
try:
    body = cq.Workplane("XY").add(body.val().fillet(RIM_EDGE_R, rim_edges))
except Exception:
    pass  # keep the sharp rim if the round-over cannot be built

# ---------------- internal thread (single helical groove) ----------------
helix = cq.Wire.makeHelix(
    pitch=THREAD_PITCH,
    height=THREAD_TURNS * THREAD_PITCH,
    radius=THREAD_MINOR,
    center=cq.Vector(0, THREAD_START, 0),
    dir=cq.Vector(0, 1, 0),
)
depth = THREAD_MAJOR - THREAD_MINOR
groove = (
    cq.Workplane(cq.Plane(origin=(0, THREAD_START, THREAD_MINOR), xDir=(0, 0, 1), normal=(1, 0, 0)))
    .polyline([
        (-0.5, -THREAD_GROOVE_W / 2),
        (depth, -THREAD_ROOT_W / 2),
        (depth, THREAD_ROOT_W / 2),
        (-0.5, THREAD_GROOVE_W / 2),
    ])
    .close()
    .sweep(cq.Workplane().add(helix), isFrenet=True)
)
body = body.cut(groove)

# ---------------- swirl slots ----------------
# each slot is a stadium sketched on a plane normal to the radial direction through the
# slot centre (a plane parallel to XY for the slot on top), inclined to the circumferential
# direction, and cut radially through the wall; then patterned around the axis.
z_top = R_LARGE + 5.0
slot_tool = (
    cq.Workplane("XY", origin=(0, 0, z_top))
    .center(0, SLOT_YC)
    .transformed(rotate=(0, 0, SLOT_ANGLE))
    .slot2D(SLOT_SPAN + SLOT_W, SLOT_W, 0)
    .extrude(-(z_top - 8.0))
)
tools = None
for i in range(N_SLOTS):
    t = slot_tool.rotate((0, 0, 0), (0, 1, 0), i * 360.0 / N_SLOTS)
    tools = t if tools is None else tools.union(t)

cut_body = body.cut(tools).val()

# ---------------- soften the slot edges ----------------
# round over every slot edge where it meets the outer or the inner cone surface
y_lo = SLOT_YC - 0.5 * (SLOT_SPAN + SLOT_W) - 1.0
y_hi = SLOT_YC + 0.5 * (SLOT_SPAN + SLOT_W) + 1.0
slot_edges = []
for e in cut_body.Edges():
    if e.geomType() in ("LINE", "CIRCLE"):
        continue
    pm = e.positionAt(0.5)
    if not (y_lo < pm.y < y_hi):
        continue
    rr = math.hypot(pm.x, pm.z)
    if abs(rr - r_out(pm.y)) < 0.05 or abs(rr - r_in(pm.y)) < 0.05:
        slot_edges.append(e)

try:
    final = cut_body.fillet(SLOT_EDGE_R, slot_edges)
    if not final.isValid():
        final = cut_body
except Exception:
    final = cut_body  # keep sharp slot edges if the round-over cannot be built

result = cq.Workplane("XY").add(final)
